import cadquery as cq
import math

# ---- driving dimensions (mm) ----
D_OUT = 50.0          # outer diameter of the cap
H = 16.1              # overall height
BORE_DEPTH = 11.6     # depth of the internal cavity (from the open bottom)
R_BORE = 19.9         # bore radius (thread crest / minor radius)
R_CHAMF = 22.0        # radius of the lead-in chamfer at the bottom face
CHAMF_DEPTH = 0.7     # axial depth of the lead-in chamfer
PITCH = 2.6           # thread pitch
THREAD_DEPTH = 0.8    # radial depth of the round thread groove
GROOVE_W = 0.98       # groove chord width (inside the cavity) / pitch
THREAD_Z0 = -0.9      # axial position of the helix start (runs out of the bottom)
TURNS = 4.27          # number of thread turns
THREAD_PHASE = 135.0  # angular position of the helix start (deg)
SEAM_ANGLE = 45.0     # where the revolve seams are placed (deg)

R_OUT = D_OUT / 2.0

# ---- main body: revolve the half cross-section (closed top, open bottom) ----
profile = [
    (R_BORE, BORE_DEPTH),
    (R_BORE, CHAMF_DEPTH),
    (R_CHAMF, 0.0),
    (R_OUT, 0.0),
    (R_OUT, H),
    (0.0, H),
    (0.0, BORE_DEPTH),
]
body = (cq.Workplane("XZ")
        .polyline(profile).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))

# ---- internal thread: round-bottom groove swept along a helix ----
e = 0.06                        # chord sits this far inside the bore
half = GROOVE_W * PITCH / 2.0
helix = cq.Wire.makeHelix(PITCH, TURNS * PITCH, R_BORE,
                          center=cq.Vector(0, 0, THREAD_Z0))
groove = (cq.Workplane("XZ")
          .moveTo(R_BORE - e, THREAD_Z0 - half)
          .threePointArc((R_BORE + THREAD_DEPTH, THREAD_Z0),
                         (R_BORE - e, THREAD_Z0 + half))
          .close()
          .sweep(cq.Workplane().add(helix), isFrenet=True)
          .rotate((0, 0, 0), (0, 0, 1), THREAD_PHASE))

result = body.cut(groove)

VIEW = {"azimuth": 45, "elevation": 26}
